"""Face-shield headband with visor brim.

A thin vertical headband strip (tangent arc chain, ending in two outward
curls/hooks) carries, over its front half, a visor: a thick floor plate
bounded by a swept rim wall whose outer face is bulged and whose top holds
a narrow slot for the clear shield.  The rim blends into the band through
flat-topped tapers; a small bump with an engraved "V" marks the front centre.
"""
import math
import cadquery as cq
from OCP.BRepOffsetAPI import BRepOffsetAPI_MakePipeShell
from OCP.gp import gp_Dir

# ---------------- driving dimensions (mm) ----------------
H = 17.5            # band / rim height
T = 2.6             # headband strip thickness
RIM_T = 7.0         # rim wall width (top view, incl. bulge)
RIM_BULGE = 3.5     # outward bulge of the rim's outer face at mid height
FLOOR_T = 4.2       # visor floor thickness
FLOOR_FR = 0.5      # concave round between visor floor and rim inner wall
GROOVE_W = 1.2      # shield slot along the rim top
GROOVE_D = 5.0
GROOVE_U = -5.25    # slot centre, measured from the rim silhouette
LIP_DROP = 1.0      # inner lip of the slot sits lower than the outer lip

# headband centre-line: tangent arc chain (radius, turn deg), starting at the
# front centre heading -X (left half; the right half is mirrored)
BAND_Y0 = 63.75
BAND_ARCS = [(151.29, 36.525), (50.63, 39.262), (139.90, 11.33), (102.77, 54.384)]
CURL_R = 6.0        # curl centre-line radius (turns the other way)
CURL_SWEEP = 282.0  # curl sweep (deg)

# visor rim outer silhouette: tangent arc chain from the front centre, -X
RIM_Y0 = 118.37
RIM_ARCS = [(289.3, 7.73), (89.09, 74.12), (276.4, 12.0)]

WEDGE_X = -116.0    # flat-topped taper blending the rim end into the band
WEDGE_Y = -44.0     # ... starting tangentially from the band here
BUMP_W = 24.0       # front-centre bump on the band outer face
BUMP_TOP = 14.5
BUMP_H = 3.0
VNOTCH_W = 8.0      # engraved "V" centre mark on the bump: top width,
VNOTCH_H = 11.0     # height,
VNOTCH_S = 1.5      # stroke width,
VNOTCH_D = 1.0      # depth
CMARK_W = 1.2       # small vertical V-groove marking the centre on the band inner face
CMARK_D = 0.6

V = cq.Vector


def arc_chain(p0, heading_deg, arcs):
    """Tangent-continuous chain of arcs. arcs = [(R, turn_deg)], R>0 turns
    left (CCW), R<0 right (CW). Returns (list of point triples, end, heading)."""
    x, y = p0
    h = math.radians(heading_deg)
    triples = []
    for r, turn in arcs:
        sgn = 1.0 if r > 0 else -1.0
        ra = abs(r)
        cxp = x - sgn * ra * math.sin(h)
        cyp = y + sgn * ra * math.cos(h)
        a_start = math.atan2(y - cyp, x - cxp)
        dphi = sgn * math.radians(turn)
        pts = []
        for k in (0.0, 0.5, 1.0):
            a = a_start + dphi * k
            pts.append(V(cxp + ra * math.cos(a), cyp + ra * math.sin(a), 0))
        triples.append(pts)
        x, y = pts[-1].x, pts[-1].y
        h += dphi
    return triples, (x, y), math.degrees(h)


def arcs_to_edges(triples, reverse=False, mirror=False):
    out = []
    seq = list(reversed(triples)) if reverse else list(triples)
    for p in seq:
        q = [V(-v.x, v.y, 0) for v in p] if mirror else list(p)
        if reverse:
            q = q[::-1]
        out.append(cq.Edge.makeThreePointArc(*q))
    return out


def prism(wire, h, z0=0.0):
    f = cq.Face.makeFromWires(wire)
    if f.normalAt().z < 0:
        f = cq.Face(f.wrapped.Reversed())
    return cq.Solid.extrudeLinear(f, V(0, 0, h)).translate(V(0, 0, z0))


def sweep_z(profile, path):
    """Sweep a profile along a planar XY path keeping it vertical (binormal Z)."""
    mk = BRepOffsetAPI_MakePipeShell(path.wrapped)
    mk.SetMode(gp_Dir(0, 0, 1))
    mk.Add(profile.wrapped, False, False)
    mk.Build()
    mk.MakeSolid()
    return cq.Solid(mk.Shape()).fix()


# ---------------- headband ----------------
bandL_t, entry_L, head_L = arc_chain((0.0, BAND_Y0), 180.0, BAND_ARCS)
curlL_t, tip_L, _ = arc_chain(entry_L, head_L, [(-CURL_R, CURL_SWEEP)])
band_L = arcs_to_edges(bandL_t)
band_R = arcs_to_edges(bandL_t, mirror=True)
curl_L = arcs_to_edges(curlL_t)
curl_R = arcs_to_edges(curlL_t, mirror=True)

band_path = cq.Wire.assembleEdges(band_R + band_L + curl_L + curl_R)
band_outline = band_path.offset2D(T / 2.0)[0]      # round-capped strip
band = prism(band_outline, H)

# head opening (inside the band centre line), closed far below the band
yb = -200.0
head_wire = cq.Wire.assembleEdges(band_R + band_L + [
    cq.Edge.makeLine(V(entry_L[0], entry_L[1], 0), V(entry_L[0], yb, 0)),
    cq.Edge.makeLine(V(entry_L[0], yb, 0), V(-entry_L[0], yb, 0)),
    cq.Edge.makeLine(V(-entry_L[0], yb, 0), V(-entry_L[0], entry_L[1], 0)),
])
head = prism(head_wire, H + 2.0, -1.0)

# ---------------- visor rim (swept bulged wall) ----------------
rimL_t, rim_end, rim_head = arc_chain((0.0, RIM_Y0), 180.0, RIM_ARCS)
# path runs from the left end, over the front, to the right end
rim_path = cq.Wire.assembleEdges(arcs_to_edges(rimL_t, reverse=True)
                                 + arcs_to_edges(rimL_t, mirror=True))
p0 = V(rim_end[0], rim_end[1], 0)
hh = math.radians(rim_head + 180.0)             # travel direction at the start
t0 = V(math.cos(hh), math.sin(hh), 0)
n_out = V(-t0.y, t0.x, 0)                       # outward (away from the head)
Z = V(0, 0, 1)


def prof_pt(u, z):
    return p0 + n_out * u + Z * z


s = RIM_BULGE
g0 = GROOVE_U + GROOVE_W / 2.0
g1 = GROOVE_U - GROOVE_W / 2.0
prof = cq.Wire.assembleEdges([
    cq.Edge.makeLine(prof_pt(-RIM_T, 0), prof_pt(-s, 0)),
    cq.Edge.makeThreePointArc(prof_pt(-s, 0), prof_pt(0, H / 2.0), prof_pt(-s, H)),
    cq.Edge.makeLine(prof_pt(-s, H), prof_pt(g0, H)),
    cq.Edge.makeLine(prof_pt(g0, H), prof_pt(g0, H - GROOVE_D)),
    cq.Edge.makeLine(prof_pt(g0, H - GROOVE_D), prof_pt(g1, H - GROOVE_D)),
    cq.Edge.makeLine(prof_pt(g1, H - GROOVE_D), prof_pt(g1, H - LIP_DROP)),
    cq.Edge.makeLine(prof_pt(g1, H - LIP_DROP), prof_pt(-RIM_T, H - LIP_DROP)),
    cq.Edge.makeLine(prof_pt(-RIM_T, H - LIP_DROP), prof_pt(-RIM_T, FLOOR_T + FLOOR_FR)),
    cq.Edge.makeThreePointArc(
        prof_pt(-RIM_T, FLOOR_T + FLOOR_FR),
        prof_pt(-RIM_T - FLOOR_FR * (1 - math.sqrt(0.5)), FLOOR_T + FLOOR_FR * (1 - math.sqrt(0.5))),
        prof_pt(-RIM_T - FLOOR_FR, FLOOR_T)),
    cq.Edge.makeLine(prof_pt(-RIM_T - FLOOR_FR, FLOOR_T), prof_pt(-RIM_T - FLOOR_FR, 0)),
    cq.Edge.makeLine(prof_pt(-RIM_T - FLOOR_FR, 0), prof_pt(-RIM_T, 0)),
])
rim = sweep_z(prof, rim_path).cut(head)

# visor floor: between the band centre line and the rim
rim_close = cq.Wire.assembleEdges(
    arcs_to_edges(rimL_t, reverse=True) + arcs_to_edges(rimL_t, mirror=True)
    + [cq.Edge.makeLine(V(-rim_end[0], rim_end[1], 0), V(rim_end[0], rim_end[1], 0))])
floor_outline = rim_close.offset2D(-(RIM_T + RIM_BULGE) / 2.0)[0]   # stays inside the rim
floor = prism(floor_outline, FLOOR_T).cut(head)

# flat-topped taper from the rim end down onto the band outer face:
# an arc leaving the band outer face tangentially at WEDGE_Y
arc_w = [e for e in band_L
         if min(e.startPoint().y, e.endPoint().y) <= WEDGE_Y <= max(e.startPoint().y, e.endPoint().y)][0]
cA3 = arc_w.arcCenter()
rA3 = arc_w.radius() + T / 2.0
dyw = WEDGE_Y - cA3.y
pw = (cA3.x - math.sqrt(rA3 ** 2 - dyw ** 2), WEDGE_Y)
rad = ((pw[0] - cA3.x) / rA3, (pw[1] - cA3.y) / rA3)
dw = (rad[1], -rad[0])                       # travel direction (upwards)
if dw[1] < 0:
    dw = (-dw[0], -dw[1])
qw = (WEDGE_X, rim_end[1])
wx, wy = qw[0] - pw[0], qw[1] - pw[1]
nw = (-dw[1], dw[0])
r_w = (wx * wx + wy * wy) / (2.0 * (wx * nw[0] + wy * nw[1]))
cw = (pw[0] + nw[0] * r_w, pw[1] + nw[1] * r_w)
a_p = math.atan2(pw[1] - cw[1], pw[0] - cw[0])
a_q = math.atan2(qw[1] - cw[1], qw[0] - cw[0])
da = math.atan2(math.sin(a_q - a_p), math.cos(a_q - a_p))
a_m = a_p + 0.5 * da
mw = (cw[0] + abs(r_w) * math.cos(a_m), cw[1] + abs(r_w) * math.sin(a_m))
wedge_w = cq.Wire.assembleEdges([
    cq.Edge.makeThreePointArc(V(pw[0], pw[1], 0), V(mw[0], mw[1], 0), V(qw[0], qw[1], 0)),
    cq.Edge.makeLine(V(qw[0], qw[1], 0), V(qw[0] + 3.0, qw[1], 0)),
    cq.Edge.makeLine(V(qw[0] + 3.0, qw[1], 0), V(pw[0] + 1.5, pw[1], 0)),
    cq.Edge.makeLine(V(pw[0] + 1.5, pw[1], 0), V(pw[0], pw[1], 0)),
])
wedge_L = prism(wedge_w, H)
wedge_R = wedge_L.mirror("YZ")

# small bump on the band outer face at the front centre
yb0 = BAND_Y0 + T / 2.0
bump = prism(cq.Wire.makePolygon([V(-BUMP_W / 2, yb0 - 1.0, 0), V(BUMP_W / 2, yb0 - 1.0, 0),
                                  V(BUMP_TOP / 2, yb0 + BUMP_H, 0), V(-BUMP_TOP / 2, yb0 + BUMP_H, 0)],
                                 close=True), H)
yv = yb0 + BUMP_H - VNOTCH_D              # engraving floor
for sx in (-1.0, 1.0):                       # the two strokes of the "V" mark
    stroke = cq.Wire.makePolygon(
        [V(sx * (VNOTCH_W / 2 + VNOTCH_S / 2), yv, H + 0.01),
         V(sx * (VNOTCH_W / 2 - VNOTCH_S / 2), yv, H + 0.01),
         V(-sx * VNOTCH_S / 2, yv, H - VNOTCH_H),
         V(sx * VNOTCH_S / 2, yv, H - VNOTCH_H)], close=True)
    bump = bump.cut(cq.Solid.extrudeLinear(cq.Face.makeFromWires(stroke),
                                           V(0, VNOTCH_D + 1.0, 0)))

# centre mark: vertical V-groove in the band's inner face
yi = BAND_Y0 - T / 2.0
cmark = cq.Solid.extrudeLinear(
    cq.Face.makeFromWires(cq.Wire.makePolygon(
        [V(-CMARK_W / 2, yi - 0.5, -1.0), V(CMARK_W / 2, yi - 0.5, -1.0),
         V(CMARK_W / 2, yi, -1.0), V(0, yi + CMARK_D, -1.0), V(-CMARK_W / 2, yi, -1.0)],
        close=True)),
    V(0, 0, H + 2.0))

body = band.fuse(rim).fuse(floor).fuse(wedge_L).fuse(wedge_R).fuse(bump).cut(cmark)
result = cq.Workplane("XY").add(body.clean())
